import math
import cadquery as cq

# ---------------- driving dimensions (mm) ----------------
# Standard-size hobby servo. Output shaft points +Y, bottom cover faces -Y,
# mounting ears stick out along X, the thin direction of the case is Z.
L = 40.0            # case length (X)
W = 20.0            # case width  (Z)
Y_COVER = 1.1       # bottom cover thickness (Y = 0 .. Y_COVER)
Y_TOP = 33.1        # top of the main case
EDGE_R = 1.3        # rounding of the case edges running along Y
TOP_R = 0.4         # rounding of the case edges around the top face
COVER_CH = 1.0      # chamfer around the front rim of the bottom cover
NOTCH = 4.3         # open square notches at the corners of the bottom face
NOTCH_D = 1.6       # notch depth (from the bottom face)
SCREW_EDGE = 2.45   # screw axis distance from the case sides
SCREW_R = 1.7       # button head radius
SCREW_TOP = 0.05    # Y of the top of the screw heads
SCREW_DOME = 1.35   # rounding of the head (nearly hemispherical)

SEAM_Y = 24.4       # parting line between middle and top case
SEAM_STEP = 0.12    # top case is a hair shorter along X

EAR_Y0 = 26.7       # mounting ears
EAR_T = 2.5
EAR_X = 26.6        # ear tip position (+-X)
EAR_H = 18.8        # ear height along Z
EAR_R = 1.0
HOLE_X = 23.9
HOLE_Z = 4.95
HOLE_R = 2.3
SLOT_W = 2.5
SLOT_MOUTH_R = 0.35
RIB_T = 1.0         # small stiffening rib on the top side of each ear
RIB_H = 1.2
RIB_X = 24.1

CAP_T = 3.2         # top cap (gear cover)
CAP_HW = 8.9        # half width of the straight part of the cap (Z)
CAP_R = 9.45        # radius of the round end of the cap around the shaft
CAP_X0 = -15.1      # -X end of the cap
SHAFT_X = 9.84      # output shaft axis position
NUB_TIP = -16.9     # tip of the rounded nub at the -X end of the cap
NUB_R = 7.5
NUB_TOP = 36.2

BOSS_R = 6.47
BOSS_TOP = 37.75
RING_R = 4.95
RING_TOP = 38.4
SPL_R = 2.94
SPL_TOP = 41.8
SPL_TEETH = 25
SPL_HOLE_R = 1.15

PLAT_X1 = -2.6      # raised plateau on the -X part of the cap (full width)
PLAT_T = 0.45
LABEL_X0 = -14.1    # rectangular label recess in the plateau
LABEL_X1 = -3.2
LABEL_HZ = 7.6
LABEL_D = 0.1       # depth of the label recess
BUMP_X0 = -2.4      # D-shaped bump: flat side at BUMP_X0, round side toward +X
BUMP_X1 = 0.0
BUMP_HZ = 1.9
BUMP_T = 0.3

GROM_T = 1.6        # cable grommet on the +X face (tapered block)
GROM_Y0 = 1.07
GROM_Y1 = 5.33
GROM_HZ0 = 3.75     # half width at the case
GROM_HZ1 = 2.95     # half width at the outer face
GROM_OY0 = 1.4      # Y extent of the outer face
GROM_OY1 = 4.3

# ---------------- helpers ----------------
def box(x0, x1, y0, y1, z0, z1):
    return (cq.Workplane("XY")
            .box(x1 - x0, y1 - y0, z1 - z0, centered=False)
            .translate((x0, y0, z0)))


def ycyl(r, y0, y1, x=0.0, z=0.0):
    # cylinder with axis along +Y from y0 to y1
    return (cq.Workplane("XZ", origin=(x, y0, z))
            .circle(r).extrude(-(y1 - y0)))


# ---------------- main case ----------------
lower = box(-L / 2, L / 2, Y_COVER, SEAM_Y, -W / 2, W / 2).edges("|Y").fillet(EDGE_R)
upper = (box(-L / 2 + SEAM_STEP, L / 2 - SEAM_STEP, SEAM_Y, Y_TOP, -W / 2, W / 2)
         .edges("|Y").fillet(EDGE_R))
upper = upper.faces(">Y").edges().fillet(TOP_R)
case = lower.union(upper)

# bottom cover: full outline with a chamfered front rim
cover = box(-L / 2, L / 2, 0.0, Y_COVER + 0.01, -W / 2, W / 2).edges("|Y").fillet(EDGE_R)
cover = cover.faces("<Y").edges().chamfer(COVER_CH, COVER_CH)
case = case.union(cover)

# open square notches at the four corners of the bottom face; the inner corner
# of each notch wraps concentrically around the cover screw
for sx in (-1, 1):
    for sz in (-1, 1):
        x0 = sx * L / 2
        z0 = sz * W / 2
        xa, xb = sorted((x0 + sx * 2.0, x0 - sx * NOTCH))
        za, zb = sorted((z0 + sz * 2.0, z0 - sz * NOTCH))
        notch = box(xa, xb, -1.0, NOTCH_D, za, zb)
        notch = notch.edges("|Y").edges(
            cq.selectors.NearestToPointSelector((x0 - sx * NOTCH, 0, z0 - sz * NOTCH))
        ).fillet(NOTCH - SCREW_EDGE - 0.05)
        case = case.cut(notch)

# domed (button) head screws with a cross recess, sitting in the notches
for sx in (-1, 1):
    for sz in (-1, 1):
        cx, cz = sx * (L / 2 - SCREW_EDGE), sz * (W / 2 - SCREW_EDGE)
        head = ycyl(SCREW_R, SCREW_TOP, NOTCH_D + 0.01, cx, cz)
        head = head.faces("<Y").edges().fillet(SCREW_DOME)
        cross = (cq.Workplane("XZ", origin=(cx, SCREW_TOP - 0.1, cz))
                 .rect(1.8, 0.45).extrude(-0.55)
                 .union(cq.Workplane("XZ", origin=(cx, SCREW_TOP - 0.1, cz))
                        .rect(0.45, 1.8).extrude(-0.55)))
        head = head.cut(cross)
        case = case.union(head)

# ---------------- mounting ears ----------------
for sx in (-1, 1):
    xa, xb = sorted((sx * (L / 2 - 1.0), sx * EAR_X))
    ear = box(xa, xb, EAR_Y0, EAR_Y0 + EAR_T, -EAR_H / 2, EAR_H / 2)
    ear = ear.edges("|Y").fillet(EAR_R)
    for sz in (-1, 1):
        hole = ycyl(HOLE_R, EAR_Y0 - 1, EAR_Y0 + EAR_T + 1, sx * HOLE_X, sz * HOLE_Z)
        sa, sb = sorted((sx * HOLE_X, sx * (EAR_X + 1)))
        slot = box(sa, sb, EAR_Y0 - 1, EAR_Y0 + EAR_T + 1,
                   sz * HOLE_Z - SLOT_W / 2, sz * HOLE_Z + SLOT_W / 2)
        ear = ear.cut(hole).cut(slot)
    # round the mouths of the open slots
    for sz in (-1, 1):
        for dz in (-1, 1):
            ear = ear.edges("|Y").edges(cq.selectors.NearestToPointSelector(
                (sx * EAR_X, EAR_Y0 + EAR_T / 2, sz * HOLE_Z + dz * SLOT_W / 2))).fillet(SLOT_MOUTH_R)
    ra, rb = sorted((sx * (L / 2 - 0.5), sx * RIB_X))
    rib = box(ra, rb, EAR_Y0 + EAR_T - 0.01, EAR_Y0 + EAR_T + RIB_T, -RIB_H / 2, RIB_H / 2)
    case = case.union(ear).union(rib)

# ---------------- top cap (gear cover) ----------------
y_cap = Y_TOP + CAP_T
cap = box(CAP_X0, SHAFT_X, Y_TOP - 0.01, y_cap, -CAP_HW, CAP_HW)
cap = cap.union(ycyl(CAP_R, Y_TOP - 0.01, y_cap, SHAFT_X, 0))
cap = cap.faces(">Y").edges().fillet(0.3)
# rounded nub on the -X end of the cap
nub = ycyl(NUB_R, Y_TOP - 0.01, NUB_TOP, NUB_TIP + NUB_R, 0)
nub = nub.intersect(box(NUB_TIP - 1, CAP_X0 + 0.5, Y_TOP - 1, NUB_TOP + 1, -W, W))
case = case.union(cap).union(nub)

# raised full-width plateau on the -X part of the cap with a shallow label recess
plat = box(CAP_X0, PLAT_X1, y_cap - 0.3, y_cap + PLAT_T, -CAP_HW, CAP_HW)
plat = plat.faces(">Y").edges().fillet(0.3)
case = case.union(plat)
case = case.cut(box(LABEL_X0, LABEL_X1, y_cap + PLAT_T - LABEL_D, y_cap + 1, -LABEL_HZ, LABEL_HZ))
# small D-shaped bump between the label and the output boss
bump_r = BUMP_HZ
bump_c = BUMP_X1 - bump_r
bump = (cq.Workplane("XZ", origin=(0, y_cap - 0.01, 0))
        .moveTo(BUMP_X0, -BUMP_HZ).lineTo(bump_c, -BUMP_HZ)
        .threePointArc((BUMP_X1, 0), (bump_c, BUMP_HZ))
        .lineTo(BUMP_X0, BUMP_HZ).close()
        .extrude(-(BUMP_T + 0.01)))
bump = bump.faces(">Y").edges().fillet(0.2)
case = case.union(bump)

# output boss, ring and splined shaft
boss = ycyl(BOSS_R, y_cap - 0.01, BOSS_TOP, SHAFT_X, 0).faces(">Y").edges().fillet(0.3)
case = case.union(boss)
case = case.union(ycyl(RING_R, BOSS_TOP - 0.01, RING_TOP, SHAFT_X, 0))
spline = ycyl(SPL_R, RING_TOP - 0.01, SPL_TOP, SHAFT_X, 0)
spline = spline.faces(">Y").edges().chamfer(0.25)
for i in range(SPL_TEETH):
    a = 2 * math.pi * i / SPL_TEETH
    gx = SHAFT_X + SPL_R * math.cos(a)
    gz = SPL_R * math.sin(a)
    spline = spline.cut(ycyl(0.17, RING_TOP + 0.3, SPL_TOP + 1, gx, gz))
spline = spline.cut(ycyl(SPL_HOLE_R, SPL_TOP - 2.0, SPL_TOP + 1, SHAFT_X, 0))
case = case.union(spline)

# ---------------- cable grommet on +X face ----------------
g_cy0 = (GROM_Y0 + GROM_Y1) / 2
g_cy1 = (GROM_OY0 + GROM_OY1) / 2
grom = (cq.Workplane("YZ", origin=(L / 2, 0, 0))
        .center(g_cy0, 0).rect(GROM_Y1 - GROM_Y0, 2 * GROM_HZ0)
        .workplane(offset=GROM_T)
        .center(g_cy1 - g_cy0, 0).rect(GROM_OY1 - GROM_OY0, 2 * GROM_HZ1)
        .loft())
grom = grom.edges("not(|Y or |Z)").fillet(0.4)
grom = grom.faces(">X").edges().fillet(0.2)
grom = grom.union(box(L / 2 - 0.8, L / 2 + 0.01, GROM_Y0, GROM_Y1, -GROM_HZ0, GROM_HZ0))
case = case.union(grom)

result = case
